import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Statue: armoured, caped figure on a round stepped plinth with an emblem.
# Built in a "standing" local frame (Z up = figure height, -Y = figure front,
# helper functions take (x, F, z) with F = forward = -y), then rotated so the
# figure stands along global +Y and faces global +Z.
# ---------------------------------------------------------------------------

# ---- plinth ---------------------------------------------------------------
BASE_R = 50.0        # outer radius of plinth
BASE_H1 = 3.4        # vertical rim height
BASE_R2 = 46.2       # radius at top of bevel
BASE_H2 = 7.8        # height at top of bevel
STEP_R = 41.6        # raised step radius
BASE_H = 9.7         # total plinth height (top of step)
EMBLEM_R_OUT = 33.0  # emblem outer ring radius
EMBLEM_R_IN = 27.0   # emblem ring inner radius
EMBLEM_HUB = 9.0     # emblem hub radius
EMBLEM_DEPTH = 1.0   # emblem pocket depth
GROOVE_R = 37.5      # ring groove radius on step

# ---- figure ---------------------------------------------------------------
WAIST_Z = 79.0
HEAD_Z = 117.6      # helmet centre height
HEAD_X = -4.6
HEAD_F = 8.0        # helmet centre, forward offset
HEAD_RX = 6.2       # helmet half width
HEAD_RF = 9.6       # helmet half depth
HEAD_RZ = 8.4       # helmet half height

SABER_R = 1.0
SABER_HAND = (-29.0, -2.0, 68.0)     # (x, F, z)
SABER_TIP = (-21.0, 64.7, 20.5)

# robe sections: (cx, cF, z, width, depth, front radius, back radius, turn)
ROBE = [
    (4.5, -13.5, BASE_H - 0.5, 72.5, 39.0, 10.0, 20.0, 14.0),
    (-2.0, -7.5, 30.0, 58.5, 36.0, 8.0, 17.0, 10.0),
    (-7.1, -4.3, 55.0, 45.5, 34.0, 7.0, 16.0, 10.0),
    (-8.65, 0.0, WAIST_Z + 1.0, 35.5, 30.0, 6.0, 12.0, 10.0),
]


def P(x, f, z):
    """local point from (x, forward, height)"""
    return cq.Vector(x, -f, z)


def cyl(p1, p2, r):
    d = p2 - p1
    return cq.Solid.makeCylinder(r, d.Length, p1, d.normalized())


def cone(p1, p2, r1, r2):
    d = p2 - p1
    if abs(r1 - r2) < 1e-6:
        return cq.Solid.makeCylinder(r1, d.Length, p1, d.normalized())
    return cq.Solid.makeCone(r1, r2, d.Length, p1, d.normalized())


def sph(p, r):
    return cq.Solid.makeSphere(r, p, angleDegrees1=-90, angleDegrees2=90)


def limb(p1, p2, r1, r2):
    """tapered limb with rounded ends"""
    return cone(p1, p2, r1, r2).fuse(sph(p1, r1)).fuse(sph(p2, r2))


def box(x0, x1, f0, f1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, f1 - f0, z1 - z0,
                            cq.Vector(x0, -f1, z0))


def drect(cx, cf, z, w, d, rf, rb, rot=0.0):
    """rounded rectangle section (front corners rf, back corners rb),
    optionally turned by rot degrees (+X side swinging forward)"""
    x0, x1 = cx - w / 2, cx + w / 2
    y0, y1 = -(cf + d / 2), -(cf - d / 2)       # y0 = front, y1 = back
    V = lambda x, y: cq.Vector(x, y, z)
    s = math.sqrt(0.5)
    e = [cq.Edge.makeLine(V(x0 + rf, y0), V(x1 - rf, y0)),
         cq.Edge.makeThreePointArc(V(x1 - rf, y0),
                                   V(x1 - rf + rf * s, y0 + rf - rf * s),
                                   V(x1, y0 + rf)),
         cq.Edge.makeLine(V(x1, y0 + rf), V(x1, y1 - rb)),
         cq.Edge.makeThreePointArc(V(x1, y1 - rb),
                                   V(x1 - rb + rb * s, y1 - rb + rb * s),
                                   V(x1 - rb, y1)),
         cq.Edge.makeLine(V(x1 - rb, y1), V(x0 + rb, y1)),
         cq.Edge.makeThreePointArc(V(x0 + rb, y1),
                                   V(x0 + rb - rb * s, y1 - rb + rb * s),
                                   V(x0, y1 - rb)),
         cq.Edge.makeLine(V(x0, y1 - rb), V(x0, y0 + rf)),
         cq.Edge.makeThreePointArc(V(x0, y0 + rf),
                                   V(x0 + rf - rf * s, y0 + rf - rf * s),
                                   V(x0 + rf, y0))]
    w = cq.Wire.assembleEdges(e)
    if rot:
        c = cq.Vector(cx, -cf, z)
        w = w.rotate(c, c + cq.Vector(0, 0, 1), -rot)
    return w


def dloft(sections):
    return cq.Solid.makeLoft([drect(*s) for s in sections], False)


def ellipsoid(c, rx, rf, rz):
    """ellipsoid centred at local point c with radii along x, F, z
    (a unit sphere with a non-uniform scaling transform)"""
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
    m = cq.Matrix([[rx, 0, 0, c.x], [0, rf, 0, c.y], [0, 0, rz, c.z]])
    return s.transformGeometry(m)


def W(s):
    return cq.Workplane("XY").add(s)


# ---- plinth ---------------------------------------------------------------
base = (cq.Workplane("XZ")
        .polyline([(0, 0), (BASE_R, 0), (BASE_R, BASE_H1), (BASE_R2, BASE_H2),
                   (STEP_R, BASE_H2), (STEP_R, BASE_H), (0, BASE_H)])
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))

# ring groove on the step
groove = (cq.Workplane("XY").workplane(offset=BASE_H - 0.6)
          .circle(GROOVE_R + 0.6).circle(GROOVE_R - 0.6).extrude(1.0))
base = base.cut(groove)

# imperial-style emblem: six pockets between spokes, notched outer ring
pockets = None
for i in range(6):
    a0 = math.radians(i * 60 + 8)
    a1 = math.radians(i * 60 + 52)
    am = math.radians(i * 60 + 30)
    pol = lambda r, a: (r * math.cos(a), r * math.sin(a))
    pk = (cq.Workplane("XY").workplane(offset=BASE_H - EMBLEM_DEPTH)
          .moveTo(*pol(EMBLEM_HUB, a0))
          .lineTo(*pol(EMBLEM_R_IN, a0))
          .threePointArc(pol(EMBLEM_R_IN, am), pol(EMBLEM_R_IN, a1))
          .lineTo(*pol(EMBLEM_HUB, a1))
          .threePointArc(pol(EMBLEM_HUB, am), pol(EMBLEM_HUB, a0))
          .close().extrude(EMBLEM_DEPTH + 1))
    notch = (cq.Workplane("XY").workplane(offset=BASE_H - EMBLEM_DEPTH)
             .center(*pol(EMBLEM_R_IN + 2.5, am))
             .transformed(rotate=(0, 0, i * 60 + 30))
             .rect(5.5, 4.0).extrude(EMBLEM_DEPTH + 1))
    pk = pk.union(notch)
    pockets = pk if pockets is None else pockets.union(pk)
outer_ring_groove = (cq.Workplane("XY").workplane(offset=BASE_H - 0.5)
                     .circle(EMBLEM_R_OUT + 0.5).circle(EMBLEM_R_OUT)
                     .extrude(1.0))
base = base.cut(pockets).cut(outer_ring_groove)

# ---- figure ---------------------------------------------------------------
# cape / robe envelope with an opening at the front for the legs
robe = W(dloft(ROBE))
opening = (cq.Workplane("XZ", origin=(0, 4.0, 0))
           .polyline([(-27.0, BASE_H - 1.0), (12.0, BASE_H - 1.0),
                      (4.5, WAIST_Z - 3.0), (-16.0, WAIST_Z - 3.0)])
           .close().extrude(60.0)           # XZ normal is -Y -> toward front
           .faces(">Y").edges("not |X").fillet(7.0))
# on the saber side the cape hangs further back
right_flap_cut = W(cone(P(-42.0, 16.0, BASE_H - 1.0), P(-42.0, 16.0, 72.0),
                        24.0, 6.0))
robe = robe.cut(opening).cut(right_flap_cut)

parts = []

# upper cape between waist and shoulders
parts.append(dloft([
    (-8.0, -1.0, WAIST_Z - 1.0, 34.0, 30.0, 6.0, 12.0),
    (-6.0, 2.0, 100.0, 33.0, 24.0, 6.0, 10.0),
]))

# legs: (hip x, knee x, ankle x, hip F, knee F, ankle F); left leg forward
for (hx, kx, ax, hf, kf, af) in [(-12.5, -18.0, -18.0, 7.5, 5.0, 5.0),
                                 (1.0, 5.0, 6.0, 10.0, 15.5, 18.5)]:
    parts.append(limb(P(hx, hf, WAIST_Z - 4), P(kx, kf, 44.0), 6.0, 5.3))
    parts.append(limb(P(kx, kf, 44.0), P(ax, af, 17.0), 5.0, 4.2))
# left boot (stepping forward), side profile extruded across its width
BOOT = [(12.0, BASE_H - 0.3), (35.5, BASE_H - 0.3), (35.5, 11.5),
        (31.0, 14.5), (24.0, 18.5), (12.0, 19.5)]
boot_l = (cq.Workplane("YZ", origin=(1.0, 0, 0))
          .polyline([(-f, z) for (f, z) in BOOT]).close()
          .extrude(10.0))
parts.append(boot_l.val())
# right boot
parts.append(W(box(-22.5, -13.0, -1.0, 15.5, BASE_H - 0.2, 18.0))
             .edges(">Z").fillet(2.0).val())
# codpiece / front tabard
parts.append(W(box(-11.0, -1.0, 9.0, 17.0, 64.0, WAIST_Z))
             .edges("<Z").fillet(2.0).val())

# torso
parts.append(dloft([
    (-6.5, 5.0, WAIST_Z - 2.0, 26.0, 22.0, 5.0, 9.0),
    (-6.5, 5.0, 97.0, 28.0, 22.0, 5.0, 9.0),
    (-6.0, 5.0, 106.0, 22.0, 17.0, 5.0, 7.0),
]))
# shoulder mantle
parts.append(dloft([
    (-6.0, 3.5, 91.0, 32.0, 24.0, 6.0, 10.0),
    (-6.0, 3.5, 101.5, 34.0, 22.0, 6.0, 9.0),
    (-5.8, 4.5, 106.5, 27.0, 17.0, 5.0, 7.0),
    (-5.5, 5.0, 109.0, 16.0, 13.0, 4.0, 5.0),
]))

# belt + buckle + chest box
parts.append(dloft([
    (-6.0, 5.0, WAIST_Z, 30.0, 26.0, 5.0, 10.0),
    (-6.0, 5.0, WAIST_Z + 4.0, 30.0, 26.0, 5.0, 10.0),
]))
parts.append(box(-10.0, -2.0, 16.5, 19.5, WAIST_Z - 0.5, WAIST_Z + 4.5))
parts.append(box(-11.4, -3.6, 14.5, 17.5, 88.0, 95.0))

# neck + helmet (dome, flared skirt, face mask)
parts.append(cyl(P(-5.0, 6.0, 104.0), P(HEAD_X, 7.0, 114.0), 4.8))
parts.append(ellipsoid(P(HEAD_X, HEAD_F, HEAD_Z), HEAD_RX, HEAD_RF, HEAD_RZ))
parts.append(cone(P(HEAD_X, HEAD_F - 2.0, HEAD_Z - 0.5),
                  P(HEAD_X, HEAD_F - 2.5, HEAD_Z - 7.0), 6.6, 8.9))
mask = (W(box(HEAD_X - 5.0, HEAD_X + 5.0, HEAD_F + 1.0, HEAD_F + 9.8,
              106.5, 115.0))
        .edges("|Z").edges("<Y").chamfer(2.5))
parts.append(mask.val())

# right arm (holding the saber)
parts.append(limb(P(-18.5, 5.0, 101.0), P(-26.0, 4.0, 84.0), 4.8, 4.2))
parts.append(limb(P(-26.0, 4.0, 84.0), P(-28.5, 0.0, 73.0), 4.2, 3.4))
parts.append(W(box(-32.5, -25.8, -5.0, 1.5, 64.0, 73.0))
             .edges().fillet(1.5).val())

# left arm raised forward (fist)
parts.append(limb(P(7.0, 4.5, 102.5), P(6.0, 8.5, 95.0), 4.8, 5.1))
parts.append(limb(P(6.0, 8.5, 95.0), P(3.0, 35.5, 104.0), 5.1, 3.8))
fist = (W(box(-1.2, 6.0, 35.5, 45.5, 101.0, 110.0))
        .edges().fillet(1.8))
parts.append(fist.val())
fingers = (W(box(-0.3, 5.3, 40.0, 47.5, 107.5, 112.3))
           .edges().fillet(1.0))
parts.append(fingers.val())

# lightsaber: hilt + blade
hand = P(*SABER_HAND)
tip = P(*SABER_TIP)
dvec = (tip - hand).normalized()
parts.append(cyl(hand - dvec * 4.0, hand + dvec * 6.0, 1.6))
parts.append(cyl(hand, tip, SABER_R))
parts.append(sph(tip, SABER_R))

fig = robe
for s in parts:
    fig = fig.union(W(s))

statue = base.union(fig)

# stand the statue along +Y, facing +Z
result = statue.rotate((0, 0, 0), (1, 0, 0), -90)

VIEW = {"azimuth": 45, "elevation": 26}
